import cadquery as cq
import math

# ======================= driving dimensions (mm) =======================
L = 93.0            # plate length (X)
W = 31.8            # plate width (Y)
T = 7.0             # plate thickness (Z)
PITCH = 8.0         # stud pitch
STUD_D = 4.8        # stud diameter
STUD_H = 2.2        # stud height
X_COL0 = 4.5        # first stud column from the left end
EDGE_ROW = 3.9      # stud row centre from the long edges

# underside cavity
WALL = 1.2          # perimeter wall thickness
CEIL = 4.5          # cavity ceiling height (top skin = T - CEIL)

# thin stud panel at the left end (flush, outlined by a shallow step)
PAN_X0, PAN_X1 = 3.55, 16.7
PAN_HW = 9.5
PAN_STEP = 0.0      # panel is flush with the plate top
PAN_T = 0.75        # panel skin thickness

# through opening and the rebated ledge along it
OPN_X0, OPN_X1 = 16.7, 41.3
OPN_HW = 9.2
LEDGE_HW = 9.5
LEDGE_D = 1.0
LEDGE_T = 0.6       # ledge skin thickness (pocketed from below)
# latch pocket between opening and slide frame (curved end)
LAT_XC, LAT_R = 26.0, 21.7     # arc centre / radius of the curved end
NOTCH_HW = 2.3
TAB_Z0, TAB_Z1 = 3.3, 4.5

# holes
HOLE_L_X, HOLE_L_D = 7.3, 4.5
HOLE_R_X, HOLE_R_D = 81.0, 4.8

# slide frame (raised U with undercut T-slot channel, open towards +X)
FR_X0, FR_X1 = 51.2, 76.2
FR_HW0, FR_HW1 = 12.1, 14.4
FR_H = 5.0
FR_R0, FR_R1 = 5.0, 4.4
CH_X0 = 56.3        # closed end of the channel (floor level)
CH_TOP_HW = 6.3     # opening between the lips
CH_UC_HW = 9.6      # undercut half width
CH_UC_Z0, CH_UC_Z1 = 1.25, 3.3   # undercut band (above plate top)
CH_BOT_HW = 7.65    # channel floor half width


# underside details
RAIL_Y, RAIL_T = -10.3, 1.2
RAIL_X0, RAIL_X1 = 41.3, 74.0
CR_X0, CR_X1 = 48.0, 87.3      # twin central rails under the slide frame
CR_Y0, CR_Y1, CR_Z0 = 2.5, 5.9, 0.7
TUBE_X, TUBE_Y = 78.3, 9.5
TUBE_OD, TUBE_ID = 6.0, 3.5
END_X = 87.3
SMALL_D, SMALL_DEPTH = 3.0, 2.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(x1 - x0, y1 - y0).extrude(z1 - z0))


def cyl(x, y, d, z0, z1):
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(d / 2).extrude(z1 - z0)


# ======================= base plate =======================
plate = box(0, L, -W / 2, W / 2, 0, T)

# hollow underside
plate = plate.cut(box(WALL, L - WALL, -W / 2 + WALL, W / 2 - WALL, -1, CEIL))
# solid end block at the right end
plate = plate.union(box(END_X, L - WALL / 2, -W / 2 + WALL / 2, W / 2 - WALL / 2, 0, CEIL + 0.01))

# thin panel under the left stud field
plate = plate.cut(box(PAN_X0, PAN_X1, -PAN_HW, PAN_HW, CEIL - 0.01, T - PAN_STEP - PAN_T))
if PAN_STEP > 0:
    plate = plate.cut(box(PAN_X0, PAN_X1, -PAN_HW, PAN_HW, T - PAN_STEP, T + 1))

# rebated ledge along the opening and the latch pocket
arc_mid = LAT_XC + LAT_R
arc_end_x = LAT_XC + math.sqrt(LAT_R ** 2 - LEDGE_HW ** 2)
led = (cq.Workplane("XY").workplane(offset=T - LEDGE_D)
       .moveTo(OPN_X0, -LEDGE_HW).lineTo(arc_end_x, -LEDGE_HW)
       .threePointArc((arc_mid, 0), (arc_end_x, LEDGE_HW))
       .lineTo(OPN_X0, LEDGE_HW).close().extrude(LEDGE_D + 1))
plate = plate.cut(led)

# pocket under the ledges (thin skin along the opening)
plate = plate.cut(box(PAN_X1 - 0.01, OPN_X1, -LEDGE_HW, LEDGE_HW, CEIL - 0.01, T - LEDGE_D - LEDGE_T))

# through opening
plate = plate.cut(box(OPN_X0, OPN_X1, -OPN_HW, OPN_HW, -1, T + 1))
# latch pocket: open down into the cavity between opening and curved wall
arc_end2 = LAT_XC + math.sqrt(LAT_R ** 2 - OPN_HW ** 2)
lat = (cq.Workplane("XY").workplane(offset=CEIL - 0.5)
       .moveTo(OPN_X1 - 0.5, -OPN_HW).lineTo(arc_end2, -OPN_HW)
       .threePointArc((arc_mid, 0), (arc_end2, OPN_HW))
       .lineTo(OPN_X1 - 0.5, OPN_HW).close().extrude(T))
plate = plate.cut(lat)
# latch tabs (two flexible tongues either side of the centre notch), rooted under the curved wall
TR = LAT_R + 1.5
tab_end = LAT_XC + math.sqrt(TR ** 2 - OPN_HW ** 2)
tabs = (cq.Workplane("XY").workplane(offset=TAB_Z0)
        .moveTo(OPN_X1, -OPN_HW).lineTo(tab_end, -OPN_HW)
        .threePointArc((LAT_XC + TR, 0), (tab_end, OPN_HW))
        .lineTo(OPN_X1, OPN_HW).close().extrude(TAB_Z1 - TAB_Z0 + 0.2))
tabs = tabs.cut(box(OPN_X1 - 1, LAT_XC + TR + 1, -NOTCH_HW, NOTCH_HW, TAB_Z0 - 1, TAB_Z1 + 1))
plate = plate.union(tabs)

# holes
plate = plate.cut(cyl(HOLE_L_X, 0, HOLE_L_D, -1, T + 1))

# ======================= underside structure =======================
plate = plate.union(box(RAIL_X0, RAIL_X1, RAIL_Y - RAIL_T / 2, RAIL_Y + RAIL_T / 2, 0, CEIL + 0.01))
for s in (1, -1):
    plate = plate.union(box(CR_X0, CR_X1, s * CR_Y0, s * CR_Y1, CR_Z0, CEIL + 0.01))
for s in (1, -1):
    tube = (cq.Workplane("XY").center(TUBE_X, s * TUBE_Y)
            .circle(TUBE_OD / 2).circle(TUBE_ID / 2).extrude(CEIL + 0.01))
    plate = plate.union(tube)
for sy in (-PITCH, 0, PITCH):
    plate = plate.cut(cyl(L - 3.0, sy, SMALL_D, -1, SMALL_DEPTH))

# ======================= studs =======================
row_y = W / 2 - EDGE_ROW
pts = []
for i in range(6):
    x = X_COL0 + i * PITCH
    pts += [(x, row_y), (x, -row_y)]
for x in (L - EDGE_ROW - PITCH, L - EDGE_ROW):
    pts += [(x, row_y), (x, -row_y)]
studs = cq.Workplane("XY").workplane(offset=T).pushPoints(pts).circle(STUD_D / 2).extrude(STUD_H)
pts_pan = [(X_COL0 + c * PITCH, y) for c in (0, 1) for y in (PITCH / 2, -PITCH / 2)]
studs2 = (cq.Workplane("XY").workplane(offset=T - PAN_STEP).pushPoints(pts_pan)
          .circle(STUD_D / 2).extrude(STUD_H + PAN_STEP))
plate = plate.union(studs).union(studs2)

# ======================= slide frame =======================
outline = [(FR_X0, -FR_HW0), (FR_X1, -FR_HW1), (FR_X1, FR_HW1), (FR_X0, FR_HW0)]
frame = cq.Workplane("XY").workplane(offset=T).polyline(outline).close().extrude(FR_H)
frame = frame.edges("|Z and <X").fillet(FR_R0)
frame = frame.edges("|Z and >X").fillet(FR_R1)

XE = FR_X1 + 2.0
# top opening between the lips
top_cut = box(CH_X0, XE, -CH_TOP_HW, CH_TOP_HW, T - 0.01, T + FR_H + 1)
# undercut profile (YZ section) swept along X
prof = [(-CH_BOT_HW, 0), (CH_BOT_HW, 0), (CH_UC_HW, CH_UC_Z0), (CH_UC_HW, CH_UC_Z1),
        (-CH_UC_HW, CH_UC_Z1), (-CH_UC_HW, CH_UC_Z0)]
uc = cq.Workplane("YZ", origin=(CH_X0, 0, T - 0.01)).polyline(prof).close().extrude(XE - CH_X0)
frame = frame.cut(top_cut).cut(uc)
result = plate.union(frame)

# right-hand through hole (also through the underside rail block)
result = result.cut(cyl(HOLE_R_X, 0, HOLE_R_D, -1, T + 1))
